import math
import cadquery as cq

# Hex head bolt (M16x1.5-like), head at the bottom, axis along +Z.
# ---------------- driving dimensions (mm) ----------------
D = 16.0              # nominal diameter = plain shank diameter
P = 1.5               # thread pitch (only used to size the simplified thread)
DT = 15.2             # thread shown as plain geometry: cylinder at ~pitch diameter
TIP_D = D - 1.0825 * P  # flat tip face = thread minor diameter (chamfered end)
S = 24.0              # hex head across flats
K = 9.5               # hex head height
H = 152.0             # overall length (head + shank + thread)
B = 72.0              # threaded length, measured from the tip
HEAD_CH_D = 0.995 * S  # head end chamfer starts just inside the across-flats circle
HEAD_CH_ANG = 17.5    # head end chamfer angle (deg, measured from the end face)
SEAM_ANG = 90.0      # where the cylinder seam lines sit (cosmetic only: on the side-view outline)

E = S / math.cos(math.radians(30))  # across corners

# ---------------- hex head (corners pointing +/-Y), outer end face at z = 0 ----------------
pts = [
    (E / 2 * math.cos(math.radians(90 + 60 * i)), E / 2 * math.sin(math.radians(90 + 60 * i)))
    for i in range(6)
]
head = cq.Workplane("XY").polyline(pts).close().extrude(K)

# shallow conical chamfer on the outer end of the head: intersect with a revolved cone body
r0 = HEAD_CH_D / 2
rmax = E / 2 + 2.0
zc = (rmax - r0) * math.tan(math.radians(HEAD_CH_ANG))
cone = (
    cq.Workplane("XZ")
    .polyline([(0, 0), (r0, 0), (rmax, zc), (rmax, K + 1), (0, K + 1)])
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)
head = head.intersect(cone)

# ---------------- shank + threaded length + 45 deg tip chamfer (one revolved profile) ----------------
ch = max((DT - TIP_D) / 2, 0.05)
prof = [(0, K - 0.5), (D / 2, K - 0.5), (D / 2, H - B)]
if abs(DT - D) > 1e-6:
    prof.append((DT / 2, H - B))
prof += [(DT / 2, H - ch), (DT / 2 - ch, H), (0, H)]
shaft = (
    cq.Workplane("XZ")
    .polyline(prof)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0), clean=False)
    .rotate((0, 0, 0), (0, 0, 1), SEAM_ANG)
)

result = head.union(shaft, clean=False)
